import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 80.0          # overall height (Z)
W = 98.8          # front plate width (X)
L = 130.0         # side plate length (Y)
TF = 10.2         # front plate thickness (Y)
TS = 6.6          # side plate thickness (X)
R_CORNER = 12.8   # rounded free-end corners of both plates

# corner gussets (top and bottom, flush with plate edges)
G_X = 68.6        # gusset reach along X measured from x=0
G_Y = 42.5        # gusset reach along Y measured from y=0
G_T = 13.0        # gusset thickness (Z)
G_FIL = 2.0       # fillet on the inner (free) diagonal edge of each gusset

# holes
HOLE_D = 5.5
CSK_D = 12.5      # 90 deg countersink diameter

# front plate bolt circle (8 holes, countersunk from inside +Y face)
FP_CX = 53.3
FP_CZ = H / 2.0 + 0.6
FP_R = 18.0
FP_N = 8
FP_START = 31.0   # deg, angle of first hole (from +X, towards +Z)

# side plate partial bolt circle (6 of 8 positions, countersunk from outside -X face)
SP_CY = 61.3
SP_CZ = H / 2.0
SP_R = 26.9
SP_ANGLES = [67.5, 112.5, 157.5, 202.5, 247.5, 292.5]  # deg from +Y towards +Z

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- plates ----------------
front = (
    cq.Workplane("XY")
    .box(W, TF, H, centered=False)
    .edges("|Y")
    .edges(">X")
    .fillet(R_CORNER)
)

side = (
    cq.Workplane("XY")
    .box(TS, L, H, centered=False)
    .edges("|X")
    .edges(">Y")
    .fillet(R_CORNER)
)

body = front.union(side)

# ---------------- gussets ----------------
# triangle in plan (legs on the inner plate faces, hypotenuse from (G_X, TF)
# to (TS, G_Y)), pushed EMB mm into both plates along the same hypotenuse
EMB = 1.0
_slope_x = (G_X - TS) / (G_Y - TF)   # dx per unit dy along the hypotenuse
tri = [
    (TS - EMB, TF - EMB),
    (G_X + EMB * _slope_x, TF - EMB),
    (TS - EMB, G_Y + EMB / _slope_x),
]


def gusset(z0, free_z):
    """Triangular corner gusset G_T thick starting at z0; the diagonal edge
    lying at height free_z (the one away from the flush face) is filleted."""
    g = cq.Workplane("XY", origin=(0, 0, z0)).polyline(tri).close().extrude(G_T).val()
    diag = []
    for e in g.Edges():
        p0, p1 = e.startPoint(), e.endPoint()
        d = p1 - p0
        on_level = abs(p0.z - free_z) < 1e-6 and abs(p1.z - free_z) < 1e-6
        if on_level and abs(d.x) > 1e-3 and abs(d.y) > 1e-3:
            diag.append(e)
    if G_FIL > 0 and diag:
        g = g.fillet(G_FIL, diag)
    return cq.Workplane("XY").add(g)


g_bot = gusset(0.0, G_T)
g_top = gusset(H - G_T, H - G_T)
body = body.union(g_bot).union(g_top)

# ---------------- holes ----------------
csk_depth = (CSK_D - HOLE_D) / 2.0  # 90 deg countersink
ext = 0.5


def csk_tool(p_face, axis, seam_dir, length):
    """Through hole + 90 deg countersink.  p_face: centre of the hole on the
    countersunk face, axis: unit vector pointing INTO the material,
    seam_dir: radial direction where the surface seams are put (hidden side)."""
    p = cq.Vector(*p_face)
    a = cq.Vector(*axis)
    cyl = cq.Solid.makeCylinder(HOLE_D / 2.0, length + 2.0, p - a * 1.0, a)
    cone = cq.Solid.makeCone(
        HOLE_D / 2.0, CSK_D / 2.0 + ext, csk_depth + ext, p + a * csk_depth, -a
    )
    tool = cyl.fuse(cone).clean()
    # rotate about the hole axis so that the seam edges sit at seam_dir
    seam = None
    for e in cone.Edges():
        if e.geomType() == "LINE":
            seam = e.Center()
    if seam is not None:
        r = seam - p
        r = r - a * r.dot(a)
        sd = cq.Vector(*seam_dir)
        sd = sd - a * sd.dot(a)
        ang = math.degrees(math.atan2(r.cross(sd).dot(a), r.dot(sd)))
        tool = tool.rotate(p, p + a, ang)
    return tool


tools = []
for i in range(FP_N):
    t = math.radians(FP_START + i * 360.0 / FP_N)
    x = FP_CX + FP_R * math.cos(t)
    z = FP_CZ + FP_R * math.sin(t)
    tools.append(csk_tool((x, TF, z), (0, -1, 0), (-1, 0, 1), TF))

for ang in SP_ANGLES:
    t = math.radians(ang)
    y = SP_CY + SP_R * math.cos(t)
    z = SP_CZ + SP_R * math.sin(t)
    tools.append(csk_tool((0.0, y, z), (1, 0, 0), (0, 1, 1), TS))

body = body.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(tools)))

# single clean solid
result = cq.Workplane("XY").add(body.solids().vals()[0])
